import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 120.0          # overall width  (X)
H = 66.1           # overall height (Z)
D = 13.8           # overall depth  (Y)  front face at Y=0, open back at Y=D

R_BOT = 5.0        # large round on the bottom/front edge
Z_FRONT = 58.3     # top edge of the flat front face
BEAD_R = 5.4       # radius of the rolled bead at the top
BEAD_TOP_Y = 11.2  # Y where the bead runs tangentially into the flat top
BEAD_START = 160.0 # polar angle (deg) where the bead arc meets the valley
# design points of the shoulder / valley curve (Y, Z) between the front edge and the bead
SHOULDER_PTS = [(1.3, 59.0), (3.4, 59.7), (4.8, 60.45)]
SHOULDER_DIR = (1.0, 0.6)  # start tangent of the shoulder at the sharp front edge
R_END = 1.5        # round on the end-face perimeter

T_WALL = 1.4       # side / bottom wall thickness
T_FRONT = 1.6      # front plate thickness
Z_TOP_IN = 57.0    # underside of the solid top (bead) region

# top vent slots (open to the back)
TOP_N = 13
TOP_PITCH = 8.1
TOP_W = 5.2
TOP_L = 2.7        # slot depth measured from the back face
TOP_R = 0.8        # corner round at the closed end of the slots
POCKET_W = 4.0     # blind pocket in each end block of the top rail
POCKET_SKIN = 1.5

# bottom vent slots (slanted comb, open to the back)
BOT_PITCH = 5.0
BAR_D = 1.9        # diameter of the comb bars
BOT_N_SIDE = 9
BOT_FIRST = 10.0   # X of the innermost slot of each group (at mid depth)
BOT_Y0 = 5.3       # slots run from here to the back
BOT_ANGLE = 36.0   # slant of the slots in the XY plane (deg from Y)
NOTCH_W = 10.7     # central notch in the bottom wall
NOTCH_L = 5.2

# mounting holes
HOLE_DX = 4.3      # hole centre from the side faces
HOLE_Z = (14.6, 51.2)
HOLE_D = 2.8
CB_D = 5.4
CB_DEPTH = 2.0
PAD_D = 7.0        # round pad behind each hole on the inside of the front plate
PAD_T = 1.0
BOSS_R = 3.0       # half width of the boss blocks (X)
BOSS_H = 7.0       # height of the boss blocks (Z)
BOSS_Y = 12.3      # boss end (from the front face)


# ---------------- helpers ----------------
def _unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def _arc_mid(c, r, p, q):
    u = _unit(((p[0] - c[0]) + (q[0] - c[0]), (p[1] - c[1]) + (q[1] - c[1])))
    return (c[0] + r * u[0], c[1] + r * u[1])


class _Sel(cq.Selector):
    def __init__(self, fn):
        self.fn = fn

    def filter(self, objs):
        return [o for o in objs if self.fn(o)]


# ---------------- outer profile (Y,Z) ----------------
# front face -> convex shoulder -> concave valley (one smooth curve) -> rolled bead arc
Ob = (BEAD_TOP_Y, H - BEAD_R)                     # bead centre
th = math.radians(BEAD_START)
P = (Ob[0] + BEAD_R * math.cos(th), Ob[1] + BEAD_R * math.sin(th))
P_dir = (math.sin(th), -math.cos(th))              # tangent of the bead arc at P
T = (BEAD_TOP_Y, H)
Ofil = (R_BOT, R_BOT)
prof = (
    cq.Workplane("YZ")
    .moveTo(0, R_BOT)
    .lineTo(0, Z_FRONT)
    .spline(SHOULDER_PTS + [P], tangents=[SHOULDER_DIR, P_dir], includeCurrent=True)
    .threePointArc(_arc_mid(Ob, BEAD_R, P, T), T)
    .lineTo(D, H)
    .lineTo(D, 0)
    .lineTo(R_BOT, 0)
    .threePointArc(_arc_mid(Ofil, R_BOT, (R_BOT, 0), (0, R_BOT)), (0, R_BOT))
    .close()
)
body = prof.extrude(W).translate((-W / 2, 0, 0))


# round the perimeter of both end faces, except the edges on the open back
def _end_edge(e):
    bb = e.BoundingBox()
    on_end = abs(bb.xmax - bb.xmin) < 1e-3 and abs(abs(bb.xmin) - W / 2) < 1e-3
    return on_end and bb.ymin < D - 1e-3


body = body.edges(_Sel(_end_edge)).fillet(R_END)

# ---------------- cavity (open to the back) ----------------
cav_w = W - 2 * T_WALL
cav = (
    cq.Workplane("XY")
    .box(cav_w, D + 2 - T_FRONT, Z_TOP_IN - T_WALL, centered=(True, False, False))
    .translate((0, T_FRONT, T_WALL))
)
cav = cav.edges("|X and <Y and <Z").fillet(R_BOT - T_WALL)
cav = cav.edges("|Z and <Y").fillet(1.0)
body = body.cut(cav)

# ---------------- screw bosses ----------------
boss_len = BOSS_Y - T_FRONT + 0.5
for sx in (-1, 1):
    hx = sx * (W / 2 - HOLE_DX)
    x_wall = sx * (W / 2 - T_WALL / 2)
    # lower boss: block from the side wall to the hole axis (the hole leaves a U channel)
    zl = HOLE_Z[0]
    blk_l = (
        cq.Workplane("XY")
        .box(abs(x_wall - hx), boss_len, BOSS_H, centered=(False, False, True))
        .translate((min(hx, x_wall), T_FRONT - 0.5, zl))
    )
    # upper boss: same U-channel block
    zu = HOLE_Z[1]
    blk_u = (
        cq.Workplane("XY")
        .box(abs(x_wall - hx), boss_len, BOSS_H, centered=(False, False, True))
        .translate((min(hx, x_wall), T_FRONT - 0.5, zu))
    )
    body = body.union(blk_l).union(blk_u)
    for hz in HOLE_Z:
        pad = (
            cq.Workplane("XZ", origin=(hx, T_FRONT - 0.2, hz))
            .circle(PAD_D / 2)
            .extrude(-(PAD_T + 0.2))
        )
        body = body.union(pad)

# ---------------- mounting holes (counterbored from the front) ----------------
for sx in (-1, 1):
    hx = sx * (W / 2 - HOLE_DX)
    for hz in HOLE_Z:
        cb = (
            cq.Workplane("XZ", origin=(hx, -0.01, hz))
            .circle(CB_D / 2)
            .extrude(-(CB_DEPTH + 0.01))
        )
        th = (
            cq.Workplane("XZ", origin=(hx, 0, hz))
            .circle(HOLE_D / 2)
            .extrude(-(BOSS_Y + 1))
        )
        body = body.cut(cb).cut(th)

# ---------------- top vent slots ----------------
for i in range(TOP_N):
    x = (i - (TOP_N - 1) / 2) * TOP_PITCH
    s = (
        cq.Workplane("XY")
        .box(TOP_W, TOP_L + 1, H - Z_TOP_IN + 2, centered=(True, False, False))
        .edges("|Z and <Y")
        .fillet(TOP_R)
        .translate((x, D - TOP_L, Z_TOP_IN - 1))
    )
    body = body.cut(s)

# blind pockets in the two end blocks of the top rail (open to back and bottom)
for sx in (-1, 1):
    x_in = sx * (W / 2 - T_WALL)
    p = (
        cq.Workplane("XY")
        .box(POCKET_W, TOP_L + 1, H - POCKET_SKIN - Z_TOP_IN + 1, centered=(False, False, False))
        .edges("|Z and <Y")
        .fillet(TOP_R)
        .translate((x_in if sx < 0 else x_in - POCKET_W, D - TOP_L, Z_TOP_IN - 1))
    )
    body = body.cut(p)

# ---------------- bottom comb: slanted round bars, open to the back ----------------
tan_a = math.tan(math.radians(BOT_ANGLE))
y_back = D + 1.0
y_mid = 0.5 * (BOT_Y0 + D)
dvec = cq.Vector(-math.sin(math.radians(BOT_ANGLE)), math.cos(math.radians(BOT_ANGLE)), 0)
for sx in (-1, 1):
    # open window spanning the whole group (slanted sides)
    x_lo = BOT_FIRST - BOT_PITCH / 2
    x_hi = BOT_FIRST + (BOT_N_SIDE - 1) * BOT_PITCH + BOT_PITCH / 2
    pts = []
    for xm, yy in ((x_lo, BOT_Y0), (x_hi, BOT_Y0), (x_hi, y_back), (x_lo, y_back)):
        pts.append((sx * xm + (y_mid - yy) * tan_a, yy))
    win = cq.Workplane("XY").workplane(offset=-1).polyline(pts).close().extrude(T_WALL + 1.3)
    body = body.cut(win)
    # round bars
    for k in range(BOT_N_SIDE):
        xm = sx * (BOT_FIRST + k * BOT_PITCH)
        y0 = BOT_Y0 - 1.0
        p0 = cq.Vector(xm + (y_mid - y0) * tan_a, y0, BAR_D / 2)
        L = (D + 2.0 - y0) / math.cos(math.radians(BOT_ANGLE))
        bar = cq.Solid.makeCylinder(BAR_D / 2, L, p0, dvec)
        body = body.union(cq.Workplane("XY").add(bar))

# trim the bars flush with the open back
trim = cq.Workplane("XY").box(W + 10, 10, 10, centered=(True, False, False)).translate((0, D, -2))
body = body.cut(trim)

notch = (
    cq.Workplane("XY")
    .box(NOTCH_W, NOTCH_L + 1, T_WALL + 2, centered=(True, False, False))
    .translate((0, D - NOTCH_L, -1))
)
body = body.cut(notch)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
